import math
import cadquery as cq

# ---------------- driving dimensions (mm) ----------------
W = 56.0            # overall width (X)
D = 60.0            # overall depth (Y), wall front face at Y=0
H = 55.0            # overall height (Z)
T_TOP = 6.1         # wall thickness above the plate
T_BOT = 9.1         # wall thickness below the plate
Z_PT = 30.1         # plate top surface height
Z_PB = 23.4         # plate bottom surface height
R_UP = 15.0         # upper web fillet radius
R_LO = 11.4         # lower web fillet radius
R_FRONT = 5.2       # front silhouette corner radius

CX, CY = 0.0, 33.4  # motor / central hole centre on the plate
R_SEAT = 19.3       # circular clearance cut into the upper web
D_CENTER = 11.9     # central through hole
CH_CENTER = 1.0     # chamfer on central hole

HOLE_SQ = 9.9       # half spacing of the 4 small holes
D_SMALL = 4.0
D_SMALL_CB = 7.2    # counterbore of the small holes, from below
SMALL_CB_DEPTH = 4.0

R_SLOT = 21.0       # pitch radius of the arc slots
W_SLOT = 3.6        # arc slot width
A_SLOT = 10.0       # arc slot half angle (deg)

BONE_DX, BONE_DY = 15.3, 14.1   # dog-bone centre offsets from hole centre
BONE_TIP = 6.95     # centre-to-tip half length of a dog-bone
BONE_CAP = 3.0      # length of the wide end caps
BONE_RE = 2.4       # half width of the end caps
BONE_HW = 1.52      # half width of the shaft at its waist
BONE_R_SIDE = 8.5   # radius of the concave shaft sides
BONE_R_CVX = 1.3    # convex corner rounds
BONE_R_CCV = 0.8    # concave corner rounds

NUT_DX, NUT_DY = 21.3, 19.5     # nut trap offsets from hole centre
NUT_AF = 6.2        # nut trap across flats
NUT_CH = 0.45       # chamfer round nut trap mouth
NUT_DEPTH = 3.5     # nut trap depth below plate top
D_NUT_HOLE = 2.9
R_BOSS = 6.0        # standoff boss radius under the plate
BOSS_H = 3.1
BOSS_FIL = 1.0

RIB_X = 22.5        # inner face of the side ribs under the plate
Y_RELIEF = 7.5      # wall back face between the ribs (below the plate)
R_RELIEF = 4.0      # corner radius of that relief
REC_X1 = -13.5      # underside recess on the -X side of the plate (inner edge)
REC_Y0, REC_Y1 = 17.8, 48.5     # recess front / back walls
Z_REC = 27.2        # recess ceiling (plate is thinner there)
FOOT_X0, FOOT_X1 = -25.0, -15.3 # widened rear foot on the recessed side
STRAP_Y0, STRAP_Y1 = 3.0, 9.6   # strap slot Y range
STRAP_HALF = 12.5               # strap slot half length (X)
STRAP_FIL = 1.5                 # round on the slot edge where it breaks through the web

half = W / 2

# ---------------- side profile (YZ) extruded across X ----------------
c_up = (T_TOP + R_UP, Z_PT + R_UP)
c_lo = (T_BOT + R_LO, Z_PB - R_LO)
s45 = math.sqrt(0.5)
prof = (
    cq.Workplane("YZ")
    .moveTo(0, 0)
    .lineTo(0, H)
    .lineTo(T_TOP, H)
    .lineTo(T_TOP, Z_PT + R_UP)
    .threePointArc((c_up[0] - R_UP * s45, c_up[1] - R_UP * s45), (T_TOP + R_UP, Z_PT))
    .lineTo(D, Z_PT)
    .lineTo(D, Z_PB)
    .lineTo(T_BOT + R_LO, Z_PB)
    .threePointArc((c_lo[0] - R_LO * s45, c_lo[1] + R_LO * s45), (T_BOT, Z_PB - R_LO))
    .lineTo(T_BOT, 0)
    .close()
    .extrude(half + 1.0, both=True)
)

# ---------------- plan outline (XY) ----------------
Y_FULL = 19.5        # plate edge runs at full width up to here
outline_pts = [      # right half of the wavy plate outline, front to back
    (half - 0.12, 23.5),
    (half - 0.5, 27.4),
    (half - 1.35, 31.7),
    (half - 1.75, 35.9),
    (half - 1.25, 40.2),
    (half - 0.4, 44.5),
    (half - 0.12, 49.0),
    (half - 0.25, 52.6),
    (half - 0.71, 54.5),
    (half - 1.46, 55.93),
    (half - 2.42, 57.18),
    (half - 3.67, 58.14),
    (half - 5.1, 58.89),
    (half - 6.7, 59.5),
    (17.0, D - 0.08),
    (11.0, D - 0.1),
    (7.0, D - 0.45),
    (3.5, D - 0.9),
    (0.0, D - 1.05),
]
left_pts = [(-x, y) for (x, y) in reversed(outline_pts[:-1])]
plan = (
    cq.Workplane("XY")
    .moveTo(half, -1.0)
    .lineTo(half, Y_FULL)
    .spline(outline_pts + left_pts + [(-half, Y_FULL)],
            tangents=[(0, 1), (0, -1)], includeCurrent=True)
    .lineTo(-half, -1.0)
    .close()
    .extrude(H + 2)
    .translate((0, 0, -1))
)

body = prof.intersect(plan)

# ---------------- rounded corners of the front silhouette ----------------
for sx in (-1, 1):
    for zc in (0.0, H):
        sz = 1 if zc > 0 else -1
        ccx = sx * (half - R_FRONT)
        ccz = zc - sz * R_FRONT
        blk = (
            cq.Workplane("XZ", origin=(0, D + 1, 0))
            .center(ccx + sx * (R_FRONT + 1) / 2, ccz + sz * (R_FRONT + 1) / 2)
            .rect(R_FRONT + 1, R_FRONT + 1)
            .extrude(D + 2)
        )
        cyl = (
            cq.Workplane("XZ", origin=(0, D + 1, 0))
            .center(ccx, ccz)
            .circle(R_FRONT)
            .extrude(D + 2)
        )
        body = body.cut(blk.cut(cyl))

# ---------------- relief between the side ribs under the plate ----------------
# below the plate only the two side ribs keep the full lower web; between them the
# wall is thinner (Y_RELIEF) and the web is cut away
y_far = T_BOT + R_LO + 1.0
relief = (
    cq.Workplane("XY", origin=(0, (Y_RELIEF + y_far) / 2, -1))
    .rect(2 * RIB_X, y_far - Y_RELIEF)
    .extrude(Z_PB + 1)
    .edges("|Z and <Y")
    .fillet(R_RELIEF)
)
body = body.cut(relief)

# ---------------- standoff bosses under the nut traps ----------------
nut_pts = [(CX + sx * NUT_DX, CY + sy * NUT_DY) for sx in (-1, 1) for sy in (-1, 1)]
bosses = (
    cq.Workplane("XY", origin=(0, 0, Z_PB - BOSS_H))
    .pushPoints(nut_pts)
    .circle(R_BOSS)
    .extrude(BOSS_H + 1.0)
    .faces("<Z")
    .edges()
    .fillet(BOSS_FIL)
)
body = body.union(bosses)
# the rear boss on the recessed (-X) side is widened into a foot toward the recess
foot = cq.Workplane("XY").box(
    FOOT_X1 - FOOT_X0, CY + NUT_DY - REC_Y1 + 1.0, BOSS_H + 1.0, centered=False
).translate((FOOT_X0, REC_Y1 - 1.0, Z_PB - BOSS_H))
body = body.union(foot)

# ---------------- underside recess on the -X side ----------------
recess = cq.Workplane("XY").box(
    REC_X1 + half + 2, REC_Y1 - REC_Y0, Z_REC, centered=(False, False, False)
).translate((-half - 2, REC_Y0, 0))
body = body.cut(recess)

# ---------------- circular seat clearance in the upper web ----------------
seat = (
    cq.Workplane("XY", origin=(0, 0, Z_PT))
    .center(CX, CY)
    .circle(R_SEAT)
    .extrude(H)
)
body = body.cut(seat)

# ---------------- central hole with chamfer ----------------
body = body.cut(
    cq.Workplane("XY", origin=(0, 0, -1)).center(CX, CY).circle(D_CENTER / 2).extrude(H + 2)
)
cham = cq.Solid.makeCone(
    D_CENTER / 2, D_CENTER / 2 + CH_CENTER + 0.6, CH_CENTER + 0.6,
    pnt=cq.Vector(CX, CY, Z_PT - CH_CENTER), dir=cq.Vector(0, 0, 1),
)
body = body.cut(cq.Workplane().add(cham))
cham_b = cq.Solid.makeCone(
    D_CENTER / 2 + CH_CENTER + 0.6, D_CENTER / 2, CH_CENTER + 0.6,
    pnt=cq.Vector(CX, CY, Z_PB - 0.6), dir=cq.Vector(0, 0, 1),
)
body = body.cut(cq.Workplane().add(cham_b))

# ---------------- four small holes ----------------
small_pts = [(CX + sx * HOLE_SQ, CY + sy * HOLE_SQ) for sx in (-1, 1) for sy in (-1, 1)]
body = body.cut(
    cq.Workplane("XY", origin=(0, 0, -1)).pushPoints(small_pts).circle(D_SMALL / 2).extrude(H + 2)
)
body = body.cut(
    cq.Workplane("XY", origin=(0, 0, Z_PB - 5)).pushPoints(small_pts)
    .circle(D_SMALL_CB / 2).extrude(5 + SMALL_CB_DEPTH)
)


# ---------------- arc slots (annular sectors) ----------------
def arc_slot(angle_deg):
    r_in = R_SLOT - W_SLOT / 2
    r_out = R_SLOT + W_SLOT / 2
    a0 = math.radians(angle_deg - A_SLOT)
    a1 = math.radians(angle_deg + A_SLOT)
    am = math.radians(angle_deg)

    def p(r, a):
        return (CX + r * math.cos(a), CY + r * math.sin(a))

    return (
        cq.Workplane("XY", origin=(0, 0, -1))
        .moveTo(*p(r_in, a0))
        .lineTo(*p(r_out, a0))
        .threePointArc(p(r_out, am), p(r_out, a1))
        .lineTo(*p(r_in, a1))
        .threePointArc(p(r_in, am), p(r_in, a0))
        .close()
        .extrude(H + 2)
        .edges("|Z")
        .fillet(1.0)
    )


for ang in (0.0, 90.0, 180.0):
    body = body.cut(arc_slot(ang))


# ---------------- dog-bone slots ----------------
def dog_bone(cx, cy, ang):
    """Bone-shaped slot: hour-glass shaft (concave sides) between wide flat caps."""
    t, cd, chw, shw = BONE_TIP, BONE_CAP, BONE_RE, BONE_HW
    uc = t - cd / 2
    sk = (
        cq.Sketch()
        .rect(2 * (t - cd) + 0.2, 2 * chw)
        .push([(0, shw + BONE_R_SIDE), (0, -shw - BONE_R_SIDE)])
        .circle(BONE_R_SIDE, mode="s")
        .reset()
        .push([(uc, 0), (-uc, 0)])
        .rect(cd, 2 * chw)
        .reset()
        .clean()
    )
    w = sk._faces.Faces()[0].outerWire()
    w = w.offset2D(BONE_R_CCV, "arc")[0].offset2D(-BONE_R_CCV, "arc")[0]   # concave rounds
    w = w.offset2D(-BONE_R_CVX, "arc")[0].offset2D(BONE_R_CVX, "arc")[0]   # convex rounds
    solid = (
        cq.Workplane("XY")
        .add(cq.Face.makeFromWires(w))
        .wires()
        .toPending()
        .extrude(H + 2)
        .translate((0, 0, -1))
    )
    return solid.rotate((0, 0, 0), (0, 0, 1), math.degrees(ang)).translate((cx, cy, 0))


for sx in (-1, 1):
    for sy in (-1, 1):
        bx, by = CX + sx * BONE_DX, CY + sy * BONE_DY
        radial = math.atan2(by - CY, bx - CX)
        body = body.cut(dog_bone(bx, by, radial + math.pi / 2))

# ---------------- nut traps (with mouth chamfer) + screw holes ----------------
r_hex = NUT_AF / math.sqrt(3)          # hexagon circumradius
for (nx, ny) in nut_pts:
    trap = (
        cq.Workplane("XY", origin=(nx, ny, Z_PT - NUT_DEPTH))
        .polygon(6, 2 * r_hex)
        .extrude(H)
        .rotate((nx, ny, 0), (nx, ny, 1), 30)
    )
    mouth = (
        cq.Workplane("XY", origin=(nx, ny, Z_PT - NUT_CH))
        .polygon(6, 2 * r_hex)
        .workplane(offset=NUT_CH + 1.0)
        .polygon(6, 2 * (r_hex + (NUT_CH + 1.0) * 2 / math.sqrt(3)))
        .loft()
        .rotate((nx, ny, 0), (nx, ny, 1), 30)
    )
    body = body.cut(trap)
    if ny > T_TOP + R_UP + r_hex:      # mouth chamfer only where the trap opens on the flat plate
        body = body.cut(mouth)
body = body.cut(
    cq.Workplane("XY", origin=(0, 0, -1)).pushPoints(nut_pts).circle(D_NUT_HOLE / 2).extrude(H + 2)
)

# ---------------- strap slot through the web / wall back ----------------
strap = (
    cq.Workplane("XY", origin=(0, 0, -1))
    .center(0, (STRAP_Y0 + STRAP_Y1) / 2)
    .slot2D(2 * STRAP_HALF, STRAP_Y1 - STRAP_Y0)
    .extrude(H + 2)
)
body = body.cut(strap)

# round the slot edge where it cuts through the curved upper web
z_web_top = Z_PT + R_UP + 0.05
web_edges = [
    e for e in body.edges().vals()
    if (lambda bb: bb.xmin > -STRAP_HALF - 0.5 and bb.xmax < STRAP_HALF + 0.5
        and bb.ymin > T_TOP - 0.05 and bb.ymax < STRAP_Y1 + 0.05
        and bb.zmin > Z_PT and bb.zmax < z_web_top)(e.BoundingBox())
]
body = body.newObject(web_edges).fillet(STRAP_FIL)

# soften the mouths of the two nut traps that open on the curved web
front_nuts = [(nx, ny) for (nx, ny) in nut_pts if ny < T_TOP + R_UP + r_hex]
mouth_edges = []
for e in body.edges().vals():
    bb = e.BoundingBox()
    for (nx, ny) in front_nuts:
        inside = (bb.xmin > nx - r_hex - 0.1 and bb.xmax < nx + r_hex + 0.1
                  and bb.ymin > ny - r_hex - 0.1 and bb.ymax < ny + r_hex + 0.1
                  and bb.zmin > Z_PT + 0.01)
        vertical = abs(bb.xmax - bb.xmin) < 1e-3 and abs(bb.ymax - bb.ymin) < 1e-3
        if inside and not vertical:
            mouth_edges.append(e)
try:
    body = body.newObject(mouth_edges).fillet(NUT_CH)
except Exception:
    pass

result = body
